"""Viviani double lobe ("sphericon-like" scoop pair).

Two lobes touch along a vertical seam B-T (B = seam bottom, T = seam top, |BT| = D).
Each lobe is closed by two faces that share one loop of Viviani's curve
(intersection of the sphere of radius D about B with the cylinder of diameter D
whose axis runs along Y through B and T):
  * upper face: the 45-degree right circular cone with apex T and axis along -Y
    (a concave scoop) - written as the exact biquadratic patch
        S(p, q) = T + (p^2 - q^2, -(p^2 + q^2), -2 p q)
    so that the apex is a regular corner of the face,
  * lower face: the ruled cone joining the seam bottom B to the loop.
The second lobe is the mirror image across the seam plane (XZ).

Resulting views: front = circle of diameter D, side = parabolic arch (2D wide, D high),
top = lemniscate of Gerono (2D long, D wide), both lobes meeting in a point.
"""
import math

import numpy as np
import cadquery as cq
from OCP.BRep import BRep_Builder
from OCP.BRepBuilderAPI import (BRepBuilderAPI_MakeEdge, BRepBuilderAPI_MakeSolid, BRepBuilderAPI_MakeVertex,
                                BRepBuilderAPI_MakeWire, BRepBuilderAPI_Sewing)
from OCP.BRepOffsetAPI import BRepOffsetAPI_ThruSections
from OCP.Geom import Geom_BSplineCurve, Geom_BSplineSurface
from OCP.Geom2d import Geom2d_BSplineCurve
from OCP.ShapeFix import ShapeFix_Solid
from OCP.TColgp import TColgp_Array1OfPnt, TColgp_Array1OfPnt2d, TColgp_Array2OfPnt
from OCP.TColStd import TColStd_Array1OfInteger, TColStd_Array1OfReal
from OCP.TopoDS import TopoDS, TopoDS_Face, TopoDS_Wire
from OCP.gp import gp_Pnt, gp_Pnt2d

# ---------------- driving dimensions ----------------
D = 100.0                 # seam height = front-view circle diameter = length of each lobe along Y
SEAM_X, SEAM_Y = 0.0, 0.0  # position of the vertical seam (B at z = 0, T at z = D)
TOL = 1e-7
SEW_TOL = 1e-5

VIEW = {"azimuth": 45, "elevation": 26}

B = gp_Pnt(SEAM_X, SEAM_Y, 0.0)   # seam bottom = centre of the Viviani sphere
T = gp_Pnt(SEAM_X, SEAM_Y, D)     # seam top = apex of the scoop cone


# ---------------- small NURBS helpers ----------------
def _real_arr(vals):
    a = TColStd_Array1OfReal(1, len(vals))
    for i, v in enumerate(vals):
        a.SetValue(i + 1, float(v))
    return a


def _int_arr(vals):
    a = TColStd_Array1OfInteger(1, len(vals))
    for i, v in enumerate(vals):
        a.SetValue(i + 1, int(v))
    return a


def _bernstein(funcs, deg):
    """Bernstein coefficients on [0, 1] of polynomials (given as callables) of degree <= deg."""
    s = np.linspace(0.0, 1.0, deg + 1)
    m = np.array([[math.comb(deg, i) * x ** i * (1.0 - x) ** (deg - i) for i in range(deg + 1)] for x in s])
    return [np.linalg.solve(m, np.array([f(x) for x in s])) for f in funcs]


def _rational_segments(segments, deg, dim):
    """Join rational Bezier segments (homogeneous polynomial callables, weight last) into poles/weights."""
    poles, weights = [], []
    for k, seg in enumerate(segments):
        coef = _bernstein(seg, deg)
        for i in range(0 if k == 0 else 1, deg + 1):
            w = coef[dim][i]
            poles.append([coef[j][i] / w for j in range(dim)])
            weights.append(w)
    return poles, weights


def _curve3d(segments, deg, knots):
    poles, weights = _rational_segments(segments, deg, 3)
    ap = TColgp_Array1OfPnt(1, len(poles))
    for i, p in enumerate(poles):
        ap.SetValue(i + 1, gp_Pnt(SEAM_X + p[0], SEAM_Y + p[1], p[2]))
    mults = [deg + 1] + [deg] * (len(knots) - 2) + [deg + 1]
    return Geom_BSplineCurve(ap, _real_arr(weights), _real_arr(knots), _int_arr(mults), deg)


def _curve2d(segments, deg, knots):
    poles, weights = _rational_segments(segments, deg, 2)
    ap = TColgp_Array1OfPnt2d(1, len(poles))
    for i, p in enumerate(poles):
        ap.SetValue(i + 1, gp_Pnt2d(p[0], p[1]))
    mults = [deg + 1] + [deg] * (len(knots) - 2) + [deg + 1]
    return Geom2d_BSplineCurve(ap, _real_arr(weights), _real_arr(knots), _int_arr(mults), deg)


# ---------------- Viviani loop (front lobe, y <= 0) ----------------
def loop_quartic():
    """Exact rational quartic, w = tan(theta/2) in [-1, 1]:  T -> F(0,-D,0) -> T.
    P = (-D sin(th) cos(th), -D cos(th), D sin(th)^2); homogeneous
    (-2D(w - w^3), -D(1 - w^4), 4D w^2 | (1 + w^2)^2)."""
    seg = lambda w0: [
        lambda s: -2 * D * ((w0 + s) - (w0 + s) ** 3),
        lambda s: -D * (1 - (w0 + s) ** 4),
        lambda s: 4 * D * (w0 + s) ** 2,
        lambda s: (1 + (w0 + s) ** 2) ** 2,
    ]
    return _curve3d([seg(-1.0), seg(0.0)], 4, [-1.0, 0.0, 1.0])


def _pq_segments():
    """Loop in the (p, q) plane of the scoop patch: the lemniscate lobe (p^2+q^2)^2 = 2 D p q,
    p = sqrt(2D) t/(1+t^4), q = sqrt(2D) t^3/(1+t^4);  second half mirrored (p <-> q)."""
    r = math.sqrt(2.0 * D)
    first = [lambda s: r * s, lambda s: r * s ** 3, lambda s: 1 + s ** 4]
    second = [lambda s: r * (1 - s) ** 3, lambda s: r * (1 - s), lambda s: 1 + (1 - s) ** 4]
    return first, second


def loop_octic():
    """The same loop, parametrised through the scoop patch: S(p(t), q(t)) (rational degree 8)."""
    def seg(f):
        return [
            lambda s: 2 * D * (f(s) ** 2 - f(s) ** 6),
            lambda s: -2 * D * (f(s) ** 2 + f(s) ** 6),
            lambda s: D * (1 - f(s) ** 4) ** 2,
            lambda s: (1 + f(s) ** 4) ** 2,
        ]
    # first half t = s (x > 0 side), second half t = 1 - s run backwards with x mirrored
    first = seg(lambda s: s)
    back = seg(lambda s: 1 - s)
    second = [lambda s: -back[0](s), back[1], back[2], back[3]]
    return _curve3d([first, second], 8, [0.0, 1.0, 2.0])


def scoop_surface():
    """Exact 45-degree cone (apex T, axis -Y) as a biquadratic Bezier in (p, q) in [0, sqrt(D)]^2."""
    pmax = math.sqrt(D)
    k2 = pmax * pmax
    cab = {(1, 1): 0.25, (1, 2): 0.5, (2, 1): 0.5, (2, 2): 1.0}   # Bernstein form of a*b
    cp = TColgp_Array2OfPnt(1, 3, 1, 3)
    for i in range(3):
        for j in range(3):
            a2, b2 = (1.0 if i == 2 else 0.0), (1.0 if j == 2 else 0.0)
            cp.SetValue(i + 1, j + 1, gp_Pnt(T.X() + k2 * (a2 - b2),
                                             T.Y() - k2 * (a2 + b2),
                                             T.Z() - 2.0 * k2 * cab.get((i, j), 0.0)))
    return Geom_BSplineSurface(cp, _real_arr([0.0, pmax]), _real_arr([0.0, pmax]),
                               _int_arr([3, 3]), _int_arr([3, 3]), 2, 2)


# ---------------- one lobe ----------------
def scoop_face():
    """Upper face of the front lobe (apex T is a regular corner of the patch) and its loop edge."""
    bb = BRep_Builder()
    vT = BRepBuilderAPI_MakeVertex(T).Vertex()
    first, second = _pq_segments()
    pcurve = _curve2d([first, second], 4, [0.0, 1.0, 2.0])
    edge = BRepBuilderAPI_MakeEdge(loop_octic(), vT, vT, 0.0, 2.0).Edge()
    face = TopoDS_Face()
    bb.MakeFace(face, scoop_surface(), TOL)
    bb.UpdateEdge(edge, pcurve, face, TOL)
    wire = TopoDS_Wire()
    bb.MakeWire(wire)
    bb.Add(wire, edge)
    bb.Add(face, wire)
    return face, edge


def ruled_cone_from_seam_bottom(loop_edge):
    """Lower face: straight rulings from the seam bottom B to every point of the loop."""
    loft = BRepOffsetAPI_ThruSections(False, True)
    loft.AddVertex(BRepBuilderAPI_MakeVertex(B).Vertex())
    loft.AddWire(BRepBuilderAPI_MakeWire(loop_edge).Wire())
    loft.Build()
    return cq.Shape.cast(loft.Shape()).Faces()


def close_lobe(faces):
    """Sew the upper and lower faces along their common loop and turn the shell into a solid."""
    try:
        sew = BRepBuilderAPI_Sewing(SEW_TOL)
        for f in faces:
            sew.Add(f)
        sew.Perform()
        if sew.NbFreeEdges() != 0:
            return None
        shell = TopoDS.Shell_s(sew.SewedShape())
        fix = ShapeFix_Solid(BRepBuilderAPI_MakeSolid(shell).Solid())
        fix.Perform()
        solid = cq.Solid(fix.Solid())
    except Exception:
        return None
    return solid if solid.isValid() and solid.Volume() > 0 else None


def front_lobe():
    upper, top_edge = scoop_face()
    vT = BRepBuilderAPI_MakeVertex(T).Vertex()
    # the lower face is lofted over the quartic form of the same loop (natural ruled parametrisation)
    low_edge = BRepBuilderAPI_MakeEdge(loop_quartic(), vT, vT, -1.0, 1.0).Edge()
    lobe = close_lobe([upper] + [f.wrapped for f in ruled_cone_from_seam_bottom(low_edge)])
    if lobe is None:   # fallback: loft over the very edge of the upper face
        lobe = close_lobe([upper] + [f.wrapped for f in ruled_cone_from_seam_bottom(top_edge)])
    return lobe


front = front_lobe()
back = front.mirror("XZ", (SEAM_X, SEAM_Y, 0.0))     # second lobe: mirror across the seam plane
result = cq.Workplane("XY").add(cq.Compound.makeCompound([front, back]))
